import math
import cadquery as cq

# ---------------------------------------------------------------- parameters
T = 4.4            # plate thickness
BLOCK_H = 4.9      # height of the two locating blocks above the plate
BLOCK_W = 5.5
BLOCK_L = 14.3
BLOCK_HOLE_D = 1.8
BLOCK_HOLE_DEPTH = 4.0
ROT = -12.0        # angular offset of the "local" feature frame (deg)
HOLE_D_S = 3.45    # small through holes
HOLE_D_M = 3.85
HOLE_D_L = 4.1
CB_OFF = 0.9       # underside counterbore radial offset
CB_DEPTH = 1.0     # underside counterbore depth
NOTCH_DEPTH = 2.4  # depth of the bayonet notches in the keyed bore

# image-measurement frame -> mm  (sheet pixel / 2)
def W(px, py):
    return ((px - 130.0) / 2.0, (390.0 - py) / 2.0)


# ---------------------------------------------------------------- 2D helpers
def _norm(v):
    l = math.hypot(v[0], v[1])
    return (v[0] / l, v[1] / l)


def _add(a, b, k=1.0):
    return (a[0] + b[0] * k, a[1] + b[1] * k)


def _sub(a, b):
    return (a[0] - b[0], a[1] - b[1])


def _dot(a, b):
    return a[0] * b[0] + a[1] * b[1]


def Lpx(p1, p2):
    a, b = W(*p1), W(*p2)
    return ("L", a, _norm(_sub(b, a)))


def Cpx(c, r, s):
    return ("C", W(*c), r / 2.0, s)


def Cmm(c, r, s):
    return ("C", c, r, s)


def _offset(prim, dist):
    if prim[0] == "L":
        d = prim[2]
        return ("L", _add(prim[1], (d[1], -d[0]), dist), d)
    return ("C", prim[1], prim[2] + prim[3] * dist, prim[3])


def _inter(A, B, hint):
    if A[0] == "L" and B[0] == "L":
        p, d = A[1], A[2]
        q, e = B[1], B[2]
        det = d[0] * (-e[1]) - (-e[0]) * d[1]
        r = _sub(q, p)
        t = (r[0] * (-e[1]) - (-e[0]) * r[1]) / det
        sols = [_add(p, d, t)]
    elif A[0] == "C" and B[0] == "C":
        c1, r1 = A[1], A[2]
        c2, r2 = B[1], B[2]
        dd = math.hypot(c2[0] - c1[0], c2[1] - c1[1])
        a = (r1 * r1 - r2 * r2 + dd * dd) / (2 * dd)
        h = math.sqrt(max(r1 * r1 - a * a, 0.0))
        u = _norm(_sub(c2, c1))
        v = (-u[1], u[0])
        m = _add(c1, u, a)
        sols = [_add(m, v, h), _add(m, v, -h)]
    else:
        if A[0] == "C":
            A, B = B, A
        p, d = A[1], A[2]
        c, R = B[1], B[2]
        f = _sub(p, c)
        b = 2 * _dot(f, d)
        cc = _dot(f, f) - R * R
        disc = math.sqrt(max(b * b - 4 * cc, 0.0))
        sols = [_add(p, d, (-b + disc) / 2), _add(p, d, (-b - disc) / 2)]
    return min(sols, key=lambda s: math.hypot(s[0] - hint[0], s[1] - hint[1]))


def _foot(prim, pt):
    if prim[0] == "L":
        p, d = prim[1], prim[2]
        return _add(p, d, _dot(_sub(pt, p), d))
    c, R = prim[1], prim[2]
    v = _norm(_sub(pt, c))
    return _add(c, v, R)


def _arc_mid(prim, p1, p2):
    c, R, s = prim[1], prim[2], prim[3]
    a1 = math.atan2(p1[1] - c[1], p1[0] - c[0])
    a2 = math.atan2(p2[1] - c[1], p2[0] - c[0])
    if s < 0:
        while a2 > a1:
            a2 -= 2 * math.pi
    else:
        while a2 < a1:
            a2 += 2 * math.pi
    am = 0.5 * (a1 + a2)
    return (c[0] + R * math.cos(am), c[1] + R * math.sin(am))


def segments(spec):
    """spec: list of (primitive, corner hint (mm), fillet radius (mm), kind).
    The boundary is walked with the material on the right; kind +1 puts the
    fillet centre in the material, -1 outside it, 0 = sharp corner.
    Returns the tangent-continuous chain of ('L', a, b) / ('A', a, mid, b)."""
    n = len(spec)
    corners = []
    for i in range(n):
        A, hint, r, kind = spec[i]
        B = spec[(i + 1) % n][0]
        if kind == 0 or r <= 0:
            p = _inter(A, B, hint)
            corners.append((p, p, None, 0.0))
        else:
            dist = r if kind > 0 else -r
            c = _inter(_offset(A, dist), _offset(B, dist), hint)
            corners.append((_foot(A, c), _foot(B, c), c, r))
    segs = []
    for i in range(n):
        prim = spec[i][0]
        a = corners[i - 1][1]
        b = corners[i][0]
        if prim[0] == "L":
            segs.append(("L", a, b))
        else:
            segs.append(("A", a, _arc_mid(prim, a, b), b))
        t1, t2, c, r = corners[i]
        if r > 0:
            m = _norm(_sub(((t1[0] + t2[0]) / 2, (t1[1] + t2[1]) / 2), c))
            segs.append(("A", t1, _add(c, m, r), t2))
        else:
            segs.append(None)
    return segs


def profile(spec):
    segs = [s for s in segments(spec) if s is not None]
    wp = cq.Workplane("XY").moveTo(*segs[0][1])
    for s in segs:
        if s[0] == "L":
            wp = wp.lineTo(*s[2])
        else:
            wp = wp.threePointArc(s[2], s[3])
    return wp.close()


def arc_part(seg, f0, f1):
    """Sub-arc of an ('A', a, mid, b) segment between angle fractions f0..f1."""
    (ax, ay), (mx, my), (bx, by) = seg[1], seg[2], seg[3]
    d = 2 * (ax * (my - by) + mx * (by - ay) + bx * (ay - my))
    ux = ((ax * ax + ay * ay) * (my - by) + (mx * mx + my * my) * (by - ay)
          + (bx * bx + by * by) * (ay - my)) / d
    uy = ((ax * ax + ay * ay) * (bx - mx) + (mx * mx + my * my) * (ax - bx)
          + (bx * bx + by * by) * (mx - ax)) / d
    r = math.hypot(ax - ux, ay - uy)
    a0 = math.atan2(ay - uy, ax - ux)
    am = math.atan2(my - uy, mx - ux)
    a1 = math.atan2(by - uy, bx - ux)
    # unwrap so that a0 -> am -> a1 is monotonic
    def unwrap(x, ref, sgn):
        while sgn * (x - ref) < 0:
            x += sgn * 2 * math.pi
        return x
    sgn = 1.0 if ((mx - ax) * (by - ay) - (my - ay) * (bx - ax)) > 0 else -1.0
    am = unwrap(am, a0, sgn)
    a1 = unwrap(a1, am, sgn)
    def pt(f):
        ang = a0 + (a1 - a0) * f
        return (ux + r * math.cos(ang), uy + r * math.sin(ang))
    return ("A", pt(f0), pt(0.5 * (f0 + f1)), pt(f1))


def chain_wire(segs):
    edges = []
    for s in segs:
        if s[0] == "L":
            edges.append(cq.Edge.makeLine(cq.Vector(*s[1], 0), cq.Vector(*s[2], 0)))
        else:
            edges.append(cq.Edge.makeThreePointArc(cq.Vector(*s[1], 0), cq.Vector(*s[2], 0),
                                                   cq.Vector(*s[3], 0)))
    return cq.Wire.assembleEdges(edges)


def edge_chamfer_cut(segs, c_h, c_v, extra=0.6):
    """Solid that removes a c_h x c_v chamfer along the lower outer edge that
    follows the (material-on-the-right) chain `segs`."""
    path = chain_wire(segs)
    p0 = segs[0][1]
    t3 = path.tangentAt(0.0)
    t = _norm((t3.x, t3.y))
    n_in = (t[1], -t[0])
    k = c_v / c_h
    e = extra
    pts2 = [(-e, c_v + e * k), (-e, -e), (c_h + e / k, -e)]
    pts3 = [cq.Vector(p0[0] + d * n_in[0], p0[1] + d * n_in[1], z) for d, z in pts2]
    prof = cq.Wire.makePolygon(pts3, close=True)
    return cq.Solid.sweep(prof, [], path, makeSolid=True, isFrenet=False)


# ---------------------------------------------------------------- outline
P1 = Lpx((11.9, 420), (35.05, 311.7))          # left edge
P2 = Cpx((84.44, 603.24), 306.73, -1)          # long shallow top arc
P3 = Lpx((173.7, 315), (176.7, 326.4))         # steep drop of the ear
P3b = Lpx((182.1, 332.8), (192.9, 335.2))      # short shelf
P4 = Lpx((203.6, 341.9), (242.9, 366.3))       # upper-right diagonal
P5 = Lpx((248.2, 374), (248.2, 384))           # right flat
P6 = Lpx((244.2, 394.6), (238.5, 401.5))       # inward slope
P7 = Lpx((233.6, 417), (236.2, 436.2))         # lower right edge
P8 = Lpx((205, 462.1), (170.4, 467.6))         # bottom right edge
P8b = Lpx((158, 466.7), (152.4, 466.2))        # small shoulder
P9 = Lpx((148.0, 470.1), (144.1, 475.2))       # flank of the bottom lobe
P10 = Cpx((173.9, 186.4), 299.9, -1)           # long lower-left arc

outline_spec = [
    (P1, W(36, 298), 8.0, 1),
    (P2, W(172, 309), 9.0, 1),
    (P3, W(177, 326), 2.5, -1),
    (P3b, W(195, 335.5), 3.0, 1),
    (P4, W(248, 370), 4.0, 1),
    (P5, W(248, 390), 5.0, 1),
    (P6, W(234, 413), 9.0, -1),
    (P7, W(237, 459), 10.0, 1),
    (P8, W(165, 468), 4.0, 1),
    (P8b, W(151, 466), 3.0, -1),
    (P9, W(137, 484), 11.8, 1),
    (P10, W(8, 432), 14.0, 1),
]

plate = profile(outline_spec).extrude(T)


# ---------------------------------------------------------------- underside edge chamfer
# the back-left half of the perimeter (lower-left arc, left edge, top edge)
# carries a small chamfer on its lower edge
EDGE_CH_H, EDGE_CH_V = 1.3, 1.2
_segs = segments(outline_spec)
_chain = ([arc_part(_segs[21], 0.35, 1.0)] + [_segs[i] for i in (22, 23, 0, 1, 2)]
          + [arc_part(_segs[3], 0.0, 0.55)])
plate = plate.cut(edge_chamfer_cut(_chain, EDGE_CH_H, EDGE_CH_V))

# ---------------------------------------------------------------- peanut cut-out
K = W(88.6, 383.2)                  # keyhole centre (also centre of the arched channel)
TOP_LOBE = (W(75.0, 344.3), 8.5)
BOT_LOBE = (W(60.5, 413.7), 8.6)
CH_RI, CH_RO = 13.65, 18.35         # arched channel radii about K


def peanut(off=0.0):
    tl = Cmm(TOP_LOBE[0], TOP_LOBE[1] + off, 1)
    ro = Cmm(K, CH_RO + off, 1)
    bl = Cmm(BOT_LOBE[0], BOT_LOBE[1] + off, 1)
    ri = Cmm(K, CH_RI - off, -1)
    spec = [
        (tl, W(60, 356), 5.0, 1),
        (ro, W(50, 402), 5.0, 1),
        (bl, W(68, 398), 3.0, 1),
        (ri, W(80, 360), 4.0, 1),
    ]
    return profile(spec)


plate = plate.cut(peanut().extrude(T))
plate = plate.cut(peanut(CB_OFF).extrude(CB_DEPTH))

# ---------------------------------------------------------------- keyhole
KEY_R = 7.15
KEY_LOBE_R = 3.35
KEY_LOBE_OFF = 7.0
ca, sa = math.cos(math.radians(ROT)), math.sin(math.radians(ROT))
lobe_c = (K[0] - KEY_LOBE_OFF * ca, K[1] - KEY_LOBE_OFF * sa)
key_spec = [
    (Cmm(K, KEY_R, 1), (lobe_c[0] + 2.0, lobe_c[1] + 3.0), 0.8, 1),
    (Cmm(lobe_c, KEY_LOBE_R, 1), (lobe_c[0] + 2.0, lobe_c[1] - 3.0), 0.8, 1),
]
plate = plate.cut(profile(key_spec).extrude(T))

# ---------------------------------------------------------------- big bore with underside counterbore
BORE2_C, BORE2_R = W(130.1, 355.9), 10.65
plate = plate.cut(cq.Workplane("XY").center(*BORE2_C).circle(BORE2_R).extrude(T))
plate = plate.cut(cq.Workplane("XY").center(*BORE2_C).circle(BORE2_R + CB_OFF).extrude(CB_DEPTH))

# ---------------------------------------------------------------- keyed bore with bayonet notches
BORE1_C, BORE1_R = W(111.4, 426.5), 11.75
plate = plate.cut(cq.Workplane("XY").center(*BORE1_C).circle(BORE1_R).extrude(T))
for ang, width, depth in ((180.0, 5.1, 1.4), (0.0, 5.1, 1.4), (-90.0, 2.2, 1.0)):
    a = math.radians(ang + ROT)
    notch = (
        cq.Workplane("XY")
        .workplane(offset=T - NOTCH_DEPTH)
        .center(BORE1_C[0], BORE1_C[1])
        .transformed(rotate=(0, 0, ang + ROT))
        .center(BORE1_R - 1.0, 0)
        .rect(depth + 1.0 + 0.0, width, centered=(False, True))
        .extrude(NOTCH_DEPTH + 0.1)
    )
    plate = plate.cut(notch)

# ---------------------------------------------------------------- oval slots with underside counterbore
SLOT_W, SLOT_L, SLOT_R = 13.3, 17.7, 6.0
SLOT_ROT = -9.0
for c in (W(200.95, 385.25), W(191.65, 428.85)):
    for off, h in ((0.0, T), (CB_OFF, CB_DEPTH)):
        s = (
            cq.Workplane("XY")
            .center(*c)
            .transformed(rotate=(0, 0, SLOT_ROT))
            .sketch()
            .rect(SLOT_W + 2 * off, SLOT_L + 2 * off)
            .vertices()
            .fillet(SLOT_R + off)
            .finalize()
            .extrude(h)
        )
        plate = plate.cut(s)

# ---------------------------------------------------------------- small through holes
HOLES_PX = {
    HOLE_D_S: [(89.6, 307.8), (136.8, 317.4), (59.7, 452.7), (106.5, 462.5)],
    HOLE_D_M: [(119.6, 315.0), (90.0, 457.8)],
    HOLE_D_L: [(35.2, 347.4), (25.3, 394.6), (144.9, 449.1), (222.9, 448.8),
               (237.9, 376.1), (166.2, 344.8)],
}
for dia, pts in HOLES_PX.items():
    plate = plate.cut(
        cq.Workplane("XY").pushPoints([W(*p) for p in pts]).circle(dia / 2).extrude(T)
    )

# ---------------------------------------------------------------- locating blocks
for c in (W(44.0, 373.7), W(108.9, 387.1)):
    blk = (
        cq.Workplane("XY")
        .workplane(offset=T)
        .center(*c)
        .transformed(rotate=(0, 0, ROT))
        .rect(BLOCK_W, BLOCK_L)
        .extrude(BLOCK_H)
    )
    hole = (
        cq.Workplane("XY")
        .workplane(offset=T + BLOCK_H - BLOCK_HOLE_DEPTH)
        .center(*c)
        .circle(BLOCK_HOLE_D / 2)
        .extrude(BLOCK_HOLE_DEPTH + 0.1)
    )
    plate = plate.union(blk).cut(hole)

result = plate
